import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
N_COLS = 4            # cells along X
N_ROWS = 5            # cells along Y
HOLE_X = 16.4         # top opening / cell size along X
HOLE_Y = 13.1         # top opening / cell size along Y
WEB_X = 4.0           # web between openings along X (= internal post size)
WEB_Y = 4.1           # web between openings along Y
WALL_X = 6.4          # outer wall thickness on the +/-X sides (margin)
WALL_Y = 6.45         # outer wall thickness on the +/-Y sides (margin)
HEIGHT = 10.65        # body height
FLOOR_T = 2.35        # floor thickness (window sill height)
PLATE_T = 1.4         # top plate thickness (above the windows)
CORNER_R = 4.0        # vertical corner radius of the body

BOSS_D = 4.65         # corner boss diameter
BOSS_INSET = 3.0      # boss centre distance from the outer faces
BOSS_H = 4.2          # boss height above the top plate
BOSS_HOLE_D = 2.0     # through hole in the bosses

TIE_HOLE_L = 2.3      # zip-tie hole length (along the wall)
TIE_HOLE_W = 2.8      # zip-tie hole width (across the wall)
TIE_TOP_C = 3.8       # hole centre offset from the window centre, on the sill
TIE_GAP = 0.05        # inner edge of each hole at the underside
TIE_INSET = 2.85      # hole centre distance from the outer face
TIE_SLOT_L = 5.4      # underside recess length (along the wall)
TIE_SLOT_D = 0.8      # underside recess depth

# ---------------- derived ----------------
PITCH_X = HOLE_X + WEB_X
PITCH_Y = HOLE_Y + WEB_Y
LX = 2 * WALL_X + N_COLS * HOLE_X + (N_COLS - 1) * WEB_X
LY = 2 * WALL_Y + N_ROWS * HOLE_Y + (N_ROWS - 1) * WEB_Y
WIN_Z0 = FLOOR_T
WIN_Z1 = HEIGHT - PLATE_T
WIN_H = WIN_Z1 - WIN_Z0

col_x = [(i - (N_COLS - 1) / 2.0) * PITCH_X for i in range(N_COLS)]
row_y = [(j - (N_ROWS - 1) / 2.0) * PITCH_Y for j in range(N_ROWS)]

# ---------------- main body ----------------
body = (
    cq.Workplane("XY")
    .rect(LX, LY)
    .extrude(HEIGHT)
    .edges("|Z")
    .fillet(CORNER_R)
)

# top openings (cells) down to the floor
cells = (
    cq.Workplane("XY")
    .workplane(offset=FLOOR_T)
    .pushPoints([(x, y) for x in col_x for y in row_y])
    .rect(HOLE_X, HOLE_Y)
    .extrude(HEIGHT)
)
body = body.cut(cells)

# tunnels along X (one per row) -> windows in the +/-X walls
for y in row_y:
    t = cq.Workplane("XY").box(LX + 10, HOLE_Y, WIN_H).translate((0, y, WIN_Z0 + WIN_H / 2))
    body = body.cut(t)

# tunnels along Y (one per column) -> windows in the +/-Y walls
for x in col_x:
    t = cq.Workplane("XY").box(HOLE_X, LY + 10, WIN_H).translate((x, 0, WIN_Z0 + WIN_H / 2))
    body = body.cut(t)

# ---------------- corner bosses ----------------
bx = LX / 2 - BOSS_INSET
by = LY / 2 - BOSS_INSET
corners = [(bx, by), (-bx, by), (-bx, -by), (bx, -by)]
bosses = (
    cq.Workplane("XY")
    .workplane(offset=HEIGHT)
    .pushPoints(corners)
    .circle(BOSS_D / 2)
    .extrude(BOSS_H)
)
body = body.union(bosses)
boss_holes = (
    cq.Workplane("XY")
    .workplane(offset=-1)
    .pushPoints(corners)
    .circle(BOSS_HOLE_D / 2)
    .extrude(HEIGHT + BOSS_H + 2)
)
body = body.cut(boss_holes)

# ---------------- zip-tie anchors in the window sills ----------------
# each perimeter window has a pair of slanted holes through its sill that meet
# under a small bridge: two openings on the sill, one shallow recess underneath.
def tie_cutter():
    """V-pair cutter in a local frame: u = along the wall (X), v = across (Y)."""
    e = 0.6                                  # overcut above / below the floor
    k = (TIE_TOP_C - TIE_HOLE_L / 2 - TIE_GAP) / FLOOR_T   # slant (du/dz)
    z0, z1 = -e, FLOOR_T + e
    cut = None
    for s in (1, -1):
        u_in0 = TIE_GAP + k * z0
        u_in1 = TIE_GAP + k * z1
        pts = [
            (s * u_in0, z0),
            (s * (u_in0 + TIE_HOLE_L), z0),
            (s * (u_in1 + TIE_HOLE_L), z1),
            (s * u_in1, z1),
        ]
        prism = (
            cq.Workplane("XZ")
            .polyline(pts)
            .close()
            .extrude(TIE_HOLE_W / 2, both=True)
        )
        cut = prism if cut is None else cut.union(prism)
    recess = cq.Workplane("XY").box(TIE_SLOT_L, TIE_HOLE_W, 2 * TIE_SLOT_D)
    return cut.union(recess)


base_cut = tie_cutter()
anchors = []
for x in col_x:                                   # front / back walls
    for sgn in (-1, 1):
        yc = sgn * (LY / 2 - TIE_INSET)
        anchors.append(base_cut.translate((x, yc, 0)))
for y in row_y:                                   # left / right walls
    for sgn in (-1, 1):
        xc = sgn * (LX / 2 - TIE_INSET)
        anchors.append(
            base_cut.rotate((0, 0, 0), (0, 0, 1), 90).translate((xc, y, 0)))
for a in anchors:
    body = body.cut(a)

result = body

VIEW = {"azimuth": 45, "elevation": 26}
